import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Action-camera body (GoPro style).  X = depth (lens points +X),
# Y = width, Z = height.  Body centred on the origin.
# ---------------------------------------------------------------------------
BX, BY, BZ = 21.0, 59.0, 41.0          # body depth, width, height
R_EDGE = 1.0                           # body edge fillet
TOP_CHAMFER = 0.6                      # chamfer on top edges along +/-Y faces

# lens (on +X face)
LENS_Y, LENS_Z = 14.45, 7.3            # lens axis position on +X face
BEZEL_R = 15.3                         # thin raised bezel plate radius
BEZEL_T = 0.3                          # bezel plate thickness
BEZEL_TOP_GAP = 2.25                   # bezel clipped this far from top edge
BEZEL_SIDE_GAP = 2.4                   # ... and from +Y edge
BEZEL_CORNER_R = 6.0
BARREL_R = 11.5
BARREL_L = 7.8                         # from body face to barrel front
FRONT_ROUND = 1.2                      # round on barrel front edge
GLASS_R = 7.55                         # cover glass radius
GLASS_H = 1.0                          # dome apex above barrel front face
GLASS_EDGE = 0.2                       # glass edge sits this far below front face
GLASS_GAP, GLASS_GAP_D = 0.3, 0.6      # pocket around the cover glass
NOTCH_L, NOTCH_W, NOTCH_D = 2.9, 1.2, 0.6   # side notches (+/-Y) on barrel
GROOVE_X0, GROOVE_W = 5.05, 0.95        # arc grooves on top/bottom of barrel
GROOVE_HALF_ANG, GROOVE_D = 18.0, 0.4

# +X face controls
SCREEN_C = (-17.2, 6.85)               # (Y, Z)
SCREEN_W, SCREEN_H, SCREEN_D = 13.4, 16.5, 0.8
BIG_BTN_C, BIG_BTN_D = (-17.1, -10.1), 12.25
SMALL_BTN_CS, SMALL_BTN_D = [(-6.6, -6.9), (-6.6, -14.0)], 5.25
BTN_H = 0.25

# top face
SHUTTER_C, SHUTTER_D = (0.0, -17.0), 12.2   # (X, Y), disc diameter
SHUTTER_GAP = 0.6                      # ring groove around the shutter disc
LED_TOP_C, LED_D = (4.9, -24.6), 2.6
PILL_TOP_C = (6.3, -6.2)
PILL_L, PILL_W, PILL_H = 5.0, 2.3, 0.3

# -Y face
CHAN_X1 = 3.3                          # channel width from back edge
CHAN_ZTOP, CHAN_ZBOT = 15.3, -15.1
CHAN_D = 1.4
CHAN_CORNER_R, CHAN_FLOOR_R = 1.2, 1.0
CHAN_EDGE_R = 1.3                      # convex round on the channel's +X edge
PILL_SIDE_C = (0.0, 0.2)               # (X, Z)
WIFI_C, WIFI_D = (0.0, -10.4), 5.3
WIFI_GAP = 0.4
WIFI_ARC_RS, WIFI_STROKE = (0.75, 1.3, 1.85), 0.22   # engraved icon
WIFI_ICON_DROP, WIFI_ICON_D = 1.2, 0.1

# +Y face (port door + ports), ranges are (X range, Z range)
PANEL_X = (-6.9, 7.3)
PANEL_Z = (-15.9, 5.4)
PORT_USB = ((2.4, 5.9), (-1.6, 4.4))
PORT_HDMI = ((1.9, 6.0), (-13.8, -5.7))
PORT_SD = ((-2.3, -0.9), (-14.5, -2.1))

# -X (back) face
DOOR_Y = (-26.6, 4.3)
DOOR_Z = (-19.5, 18.5)
LATCH_C = (11.0, -1.0)                 # (Y, Z)
LATCH_W, LATCH_H, LATCH_D = 5.5, 12.0, 0.8
BACK_LED_C, BACK_LED_D = (26.1, 14.1), 3.0
BACK_WIN_Y, BACK_WIN_W = 26.0, 3.4        # shallow window recess below LED
BACK_WIN_Z = (-11.6, 11.5)

# bottom
FOOT_C = (-6.0, 23.5)

hx, hy, hz = BX / 2, BY / 2, BZ / 2


def plane(face):
    """Workplane lying on a body face, normal pointing outwards."""
    if face == "+X":   # local (Y, Z)
        return cq.Workplane(cq.Plane((hx, 0, 0), (0, 1, 0), (1, 0, 0)))
    if face == "-X":   # local (-Y, Z)
        return cq.Workplane(cq.Plane((-hx, 0, 0), (0, -1, 0), (-1, 0, 0)))
    if face == "-Y":   # local (X, Z)
        return cq.Workplane(cq.Plane((0, -hy, 0), (1, 0, 0), (0, -1, 0)))
    if face == "+Y":   # local (-X, Z)
        return cq.Workplane(cq.Plane((0, hy, 0), (-1, 0, 0), (0, 1, 0)))
    if face == "+Z":   # local (X, Y)
        return cq.Workplane(cq.Plane((0, 0, hz), (1, 0, 0), (0, 0, 1)))
    if face == "-Z":   # local (X, -Y)
        return cq.Workplane(cq.Plane((0, 0, -hz), (1, 0, 0), (0, 0, -1)))
    raise ValueError(face)


def rrect(wp, w, h, r):
    """Rounded rectangle sketch on a workplane (already centred)."""
    return wp.sketch().rect(w, h).vertices().fillet(r).finalize()


# ---------------------------------------------------------------- body
body = (cq.Workplane("XY").box(BX, BY, BZ)
        .edges("|X and >Z").chamfer(TOP_CHAMFER)
        .edges("(not |X) or <Z").fillet(R_EDGE))

# vertical channel at the back corner of the -Y face (open to the back).
# Profile in XY: flat floor, wall on the +X side whose outer edge is a
# convex round, extruded along Z between the top and bottom lips.
ch_xw = -hx + CHAN_X1
ch_yf = -hy + CHAN_D
ch_c = (ch_xw + CHAN_EDGE_R, -hy + CHAN_EDGE_R)
ch_mid = (ch_c[0] - CHAN_EDGE_R * math.cos(math.radians(45)),
          ch_c[1] - CHAN_EDGE_R * math.sin(math.radians(45)))
chan = (cq.Workplane("XY", origin=(0, 0, CHAN_ZBOT))
        .moveTo(-hx - 1, -hy - 1)
        .lineTo(-hx - 1, ch_yf)
        .lineTo(ch_xw, ch_yf)
        .lineTo(ch_xw, -hy + CHAN_EDGE_R)
        .threePointArc(ch_mid, (ch_xw + CHAN_EDGE_R, -hy))
        .lineTo(ch_xw + CHAN_EDGE_R, -hy - 1)
        .close()
        .extrude(CHAN_ZTOP - CHAN_ZBOT))
chan = chan.edges("|Y").fillet(CHAN_CORNER_R)          # rounded channel ends
chan = chan.edges(cq.selectors.BoxSelector(             # floor-to-end ramps
    (-hx - 0.5, ch_yf - 0.01, CHAN_ZBOT - 1), (ch_xw - 0.01, ch_yf + 0.01, CHAN_ZTOP + 1))
).fillet(CHAN_FLOOR_R)
body = body.cut(chan)

# ---------------------------------------------------------------- +X face
screen = rrect(plane("+X").center(*SCREEN_C), SCREEN_W, SCREEN_H, 1.2).extrude(-SCREEN_D)
body = body.cut(screen)

for c, d in [(BIG_BTN_C, BIG_BTN_D)] + [(c, SMALL_BTN_D) for c in SMALL_BTN_CS]:
    b = plane("+X").center(*c).circle(d / 2).extrude(BTN_H)
    body = body.union(b.faces(">X").edges().fillet(0.2))

# thin bezel plate around the lens, clipped near the top / +Y edges
bez = plane("+X").center(LENS_Y, LENS_Z).circle(BEZEL_R).extrude(BEZEL_T)
clip = rrect(plane("+X").center(-BEZEL_SIDE_GAP / 2, -BEZEL_TOP_GAP / 2),
             BY - BEZEL_SIDE_GAP, BZ - BEZEL_TOP_GAP, BEZEL_CORNER_R).extrude(BEZEL_T)
bez = bez.intersect(clip)
# soften the two sharp junctions where the clip lines meet the circle
z_top = hz - BEZEL_TOP_GAP
y_side = hy - BEZEL_SIDE_GAP
for py, pz in ((LENS_Y - math.sqrt(BEZEL_R ** 2 - (z_top - LENS_Z) ** 2), z_top),
               (y_side, LENS_Z - math.sqrt(BEZEL_R ** 2 - (y_side - LENS_Y) ** 2))):
    bez = bez.edges(cq.selectors.NearestToPointSelector((hx + BEZEL_T / 2, py, pz))).fillet(1.5)
body = body.union(bez)

# ---------------------------------------------------------------- lens
xf = hx + BARREL_L                     # barrel front face (global X)


def lens_wp(x):
    """Workplane normal to +X centred on the lens axis at axial station x
    (x-dir points down so circle seams sit on the hidden underside)."""
    return cq.Workplane(cq.Plane((x, LENS_Y, LENS_Z), (0, 0, -1), (1, 0, 0)))


barrel = (lens_wp(hx - 0.5).circle(BARREL_R).extrude(BARREL_L + 0.5)
          .faces(">X").edges().fillet(FRONT_ROUND))
barrel = barrel.cut(lens_wp(xf - GLASS_GAP_D).circle(GLASS_R + GLASS_GAP).extrude(2.0))

# domed cover glass: cylinder capped by a large sphere
cap_h = GLASS_H + GLASS_EDGE
sph_r = (GLASS_R ** 2 + cap_h ** 2) / (2 * cap_h)
sph = (cq.Workplane("XY").sphere(sph_r)            # seam turned away from cap
       .rotate((0, 0, 0), (0, 0, 1), 180)
       .translate((xf + GLASS_H - sph_r, LENS_Y, LENS_Z)))
glass = (lens_wp(xf - GLASS_GAP_D - 0.3).circle(GLASS_R)
         .extrude(GLASS_GAP_D + 0.3 + GLASS_H + 1.0).intersect(sph))
barrel = barrel.union(glass)

# short axial notches on the +/-Y sides of the barrel, open to the front
for s in (-1, 1):
    notch = (cq.Workplane(cq.Plane((xf, LENS_Y + s * BARREL_R, LENS_Z), (1, 0, 0), (0, s, 0)))
             .center(-NOTCH_L / 2 + 0.5, 0).slot2D(NOTCH_L + 1.0, NOTCH_W)
             .extrude(-NOTCH_D, both=True))
    barrel = barrel.cut(notch)

# short arc grooves on top and bottom of the barrel
g0 = hx + GROOVE_X0
groove = (lens_wp(g0).circle(BARREL_R + 1.0).circle(BARREL_R - GROOVE_D)
          .extrude(GROOVE_W))
gbox = (cq.Workplane("XY")
        .box(GROOVE_W + 1, 2 * BARREL_R * math.sin(math.radians(GROOVE_HALF_ANG)), 4 * BARREL_R)
        .translate((g0 + GROOVE_W / 2, LENS_Y, LENS_Z)))
barrel = barrel.cut(groove.intersect(gbox))

body = body.union(barrel)

# ---------------------------------------------------------------- top face
sh_ring = (plane("+Z").center(*SHUTTER_C).circle(SHUTTER_D / 2 + SHUTTER_GAP)
           .circle(SHUTTER_D / 2).extrude(-0.3))
body = body.cut(sh_ring)
sh = plane("+Z").center(*SHUTTER_C).circle(SHUTTER_D / 2 - 0.05).extrude(0.35)
body = body.union(sh.faces(">Z").edges().fillet(0.25))

led = plane("+Z").center(*LED_TOP_C).circle(LED_D / 2).extrude(0.3)
body = body.union(led.faces(">Z").edges().fillet(0.2))


def pill(face, c):
    """Raised pill-shaped status light with three small dimples (vertical in
    the face's local y direction)."""
    res = plane(face).center(*c).slot2D(PILL_L, PILL_W, 90).extrude(PILL_H)
    for k in (-1, 0, 1):
        res = res.cut(plane(face).workplane(offset=PILL_H - 0.2)
                      .center(c[0], c[1] + k * 1.55).circle(0.55).extrude(0.5))
    return res


body = body.union(pill("+Z", PILL_TOP_C))

# ---------------------------------------------------------------- -Y face
body = body.union(pill("-Y", PILL_SIDE_C))
wifi_ring = (plane("-Y").center(*WIFI_C).circle(WIFI_D / 2 + WIFI_GAP)
             .circle(WIFI_D / 2).extrude(-0.3))
body = body.cut(wifi_ring)
wifi = plane("-Y").center(*WIFI_C).circle(WIFI_D / 2 - 0.05).extrude(0.3)
body = body.union(wifi)
# engraved wi-fi symbol: three concentric 90 deg arcs above a dot
icon_wp = plane("-Y").workplane(offset=0.3 - WIFI_ICON_D)
icx, icz = WIFI_C[0], WIFI_C[1] - WIFI_ICON_DROP
wedge = (icon_wp.center(icx, icz)
         .polyline([(0, 0), (2.5, 2.5), (0, 3.6), (-2.5, 2.5)]).close().extrude(0.5))
for r in WIFI_ARC_RS:
    arc = (icon_wp.center(icx, icz).circle(r + WIFI_STROKE / 2)
           .circle(r - WIFI_STROKE / 2).extrude(0.5))
    body = body.cut(arc.intersect(wedge))
body = body.cut(icon_wp.center(icx, icz).circle(0.22).extrude(0.5))

# ---------------------------------------------------------------- +Y face
pcx = -(PANEL_X[0] + PANEL_X[1]) / 2
pcz = (PANEL_Z[0] + PANEL_Z[1]) / 2
panel = rrect(plane("+Y").center(pcx, pcz),
              PANEL_X[1] - PANEL_X[0], PANEL_Z[1] - PANEL_Z[0], 1.2).extrude(-0.3)
body = body.cut(panel)
for (xr, zr), r in ((PORT_USB, 0.4), (PORT_HDMI, 0.8), (PORT_SD, 0.3)):
    w, h = xr[1] - xr[0], zr[1] - zr[0]
    port = rrect(plane("+Y").center(-(xr[0] + xr[1]) / 2, (zr[0] + zr[1]) / 2),
                 w, h, min(r, w / 2 - 0.05)).extrude(-2.0)
    body = body.cut(port)

# ---------------------------------------------------------------- -X face
dcy = -(DOOR_Y[0] + DOOR_Y[1]) / 2
dcz = (DOOR_Z[0] + DOOR_Z[1]) / 2
door_groove = (plane("-X").center(dcy, dcz)
               .rect(DOOR_Y[1] - DOOR_Y[0], DOOR_Z[1] - DOOR_Z[0])
               .rect(DOOR_Y[1] - DOOR_Y[0] - 1.0, DOOR_Z[1] - DOOR_Z[0] - 1.0)
               .extrude(-0.4))
body = body.cut(door_groove)

# door latch: recessed pocket with a slightly lower slider inside
latch_pocket = rrect(plane("-X").center(-LATCH_C[0], LATCH_C[1]),
                     LATCH_W, LATCH_H, 1.0).extrude(-LATCH_D)
latch_slider = rrect(plane("-X").workplane(offset=-LATCH_D - 0.1).center(-LATCH_C[0], LATCH_C[1]),
                     LATCH_W - 1.4, LATCH_H - 1.4, 0.6).extrude(LATCH_D - 0.1)
body = body.cut(latch_pocket).union(latch_slider)

back_led = (plane("-X").center(-BACK_LED_C[0], BACK_LED_C[1])
            .circle(BACK_LED_D / 2).circle(BACK_LED_D / 2 - 0.3).extrude(-0.25))
body = body.cut(back_led)
back_win = rrect(plane("-X").center(-BACK_WIN_Y, (BACK_WIN_Z[0] + BACK_WIN_Z[1]) / 2),
                 BACK_WIN_W, BACK_WIN_Z[1] - BACK_WIN_Z[0], 0.6).extrude(-0.25)
body = body.cut(back_win)

# ---------------------------------------------------------------- bottom
foot = plane("-Z").center(FOOT_C[0], -FOOT_C[1]).circle(1.0).extrude(0.3)
body = body.union(foot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
